"""Knurled heat-set threaded insert (metric 60 deg internal thread).

Two bands of 15 helical teeth (upper band right-handed, lower band
left-handed, mirror images of each other about the plain groove between
them), a plain pilot at the bottom, an internal 60 deg thread through the
whole length and a short plain lead-in counterbore at the bottom end.
Axis = Z, pilot at the bottom (z = 0), top face at z = H.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
OD = 8.2              # outer diameter over the knurl teeth
CORE_D = 6.29         # root / core diameter (also pilot & groove diameter)
N_TEETH = 15          # teeth per band
TOOTH_W_ROOT = 0.64   # tooth width (chord) at the root circle, transverse section
TOOTH_W_TIP = 0.58    # tooth width (chord) at the outer diameter
FLANK_BULGE = 0.07    # convexity (sagitta) of the tooth flanks
HELIX_DEG = 32.5      # helix angle of the teeth at the outer diameter

PILOT_H = 1.77        # plain pilot at the bottom
BAND_H = 2.08         # height of each toothed band
GAP_H = 1.16          # plain groove between the bands
TOP_PHASE = 14.5      # angle of a tooth centre on the top face (deg from +X)

THREAD_MAJOR = 6.0    # internal thread major diameter
PITCH = 1.06          # thread pitch (right hand)
THREAD_MINOR = THREAD_MAJOR - 1.0825 * PITCH  # ISO basic minor diameter
THREAD_PHASE = 64.0   # angle at which the thread root meets the top face
CB_D = 5.86           # plain lead-in counterbore at the bottom end
CB_DEPTH = 0.6

SEAM_OUT = 180.0      # where the seams of the outer cylinders are put
SEAM_IN = -135.0      # where the seams of the bore faces are put

# ---------------- derived values ----------------
H = PILOT_H + 2 * BAND_H + GAP_H
R_OUT = OD / 2.0
R_CORE = CORE_D / 2.0
# twist of one band (degrees) for the given helix angle at the outer diameter
TWIST = math.degrees(BAND_H * math.tan(math.radians(HELIX_DEG)) / R_OUT)

z_lb0 = PILOT_H               # lower band
z_lb1 = z_lb0 + BAND_H
z_ub0 = z_lb1 + GAP_H         # upper band
z_ub1 = z_ub0 + BAND_H        # == H


def cylinder(r, z0, h, seam_deg):
    """Plain cylinder on the Z axis with its seam turned to seam_deg."""
    c = cq.Solid.makeCylinder(r, h, cq.Vector(0, 0, z0), cq.Vector(0, 0, 1))
    return c.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), seam_deg)


def toothed_section(wp, phase_deg):
    """Closed transverse section: root circle with N barrel-shaped teeth."""
    pitch = 2 * math.pi / N_TEETH
    a_root = math.asin(TOOTH_W_ROOT / 2.0 / R_CORE)
    a_out = math.asin(TOOTH_W_TIP / 2.0 / R_OUT)
    ph = math.radians(phase_deg)

    def pt(r, a):
        return (r * math.cos(a), r * math.sin(a))

    def flank_mid(p, q, c, side):
        # flank midpoint pushed away from the tooth centre line by FLANK_BULGE
        mx, my = (p[0] + q[0]) / 2.0, (p[1] + q[1]) / 2.0
        tx, ty = q[0] - p[0], q[1] - p[1]
        ln = math.hypot(tx, ty)
        nx, ny = -ty / ln, tx / ln
        if (nx * -math.sin(c) + ny * math.cos(c)) * side < 0:
            nx, ny = -nx, -ny
        return (mx + FLANK_BULGE * nx, my + FLANK_BULGE * ny)

    first = None
    w = wp
    for i in range(N_TEETH):
        c = ph + i * pitch
        p_root1 = pt(R_CORE, c - a_root)
        p_tip1 = pt(R_OUT, c - a_out)
        p_tip2 = pt(R_OUT, c + a_out)
        p_root2 = pt(R_CORE, c + a_root)
        if i == 0:
            w = w.moveTo(*p_root1)
            first = p_root1
        w = w.threePointArc(flank_mid(p_root1, p_tip1, c, -1), p_tip1)   # flank
        w = w.threePointArc(pt(R_OUT, c), p_tip2)                         # tip
        w = w.threePointArc(flank_mid(p_tip2, p_root2, c, 1), p_root2)   # flank
        nxt = first if i == N_TEETH - 1 else pt(R_CORE, c + pitch - a_root)
        w = w.threePointArc(pt(R_CORE, c + pitch / 2.0), nxt)            # root
    return w.close()


def band(z0, phase_bottom, twist):
    """One helical knurl band: the section twisted while extruded."""
    wp = cq.Workplane("XY").workplane(offset=z0)
    return toothed_section(wp, phase_bottom).twistExtrude(BAND_H, twist)


# ---------------- knurled body ----------------
# upper band: right-hand helix, tooth at TOP_PHASE on the top face
upper = band(z_ub0, TOP_PHASE - TWIST, TWIST)
# lower band: left-hand helix, mirror of the upper band about the groove
lower = band(z_lb0, TOP_PHASE, -TWIST)

pilot = cq.Workplane("XY").add(cylinder(R_CORE, 0.0, PILOT_H, SEAM_OUT))
groove = cq.Workplane("XY").add(cylinder(R_CORE, z_lb1, GAP_H, SEAM_OUT))

body = pilot.union(lower).union(groove).union(upper)

# ---------------- internal thread ----------------
# through hole on the minor diameter, bottom lead-in counterbore, plus a
# helical ISO 60 deg groove (flat root P/8 on the major diameter) that is
# swept one turn at a time.
r_min = THREAD_MINOR / 2.0
r_maj = THREAD_MAJOR / 2.0
r_in = r_min - 0.1                      # groove flanks run out inside the hole
hw_root = PITCH / 16.0
hw_in = hw_root + (r_maj - r_in) * math.tan(math.radians(30.0))

body = body.cut(cq.Workplane("XY").add(cylinder(r_min, -1.0, H + 2.0, SEAM_IN)))

groove_prof = cq.Wire.makePolygon(
    [
        cq.Vector(r_in, 0, -hw_in),
        cq.Vector(r_maj, 0, -hw_root),
        cq.Vector(r_maj, 0, hw_root),
        cq.Vector(r_in, 0, hw_in),
    ],
    close=True,
)
turn_path = cq.Wire.makeHelix(PITCH, PITCH, r_min)
one_turn = (
    cq.Workplane("XZ").add(groove_prof).toPending().sweep(turn_path, isFrenet=True).val()
).rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1), SEAM_IN)

# groove centre is at angle a on z = z_g0 + P*a/360 (+k*P);
# the root meets the top face at THREAD_PHASE
z_g0 = H - PITCH * THREAD_PHASE / 360.0
z_s0 = z_g0 + PITCH * SEAM_IN / 360.0   # turn start (at SEAM_IN) for k = 0
k0 = int(math.floor((CB_DEPTH - hw_in - z_s0) / PITCH)) - 1
k1 = int(math.ceil((H + hw_in - z_s0) / PITCH)) + 1
for k in range(k0, k1):
    zs = z_s0 + k * PITCH
    if zs + PITCH + hw_in <= CB_DEPTH or zs - hw_in >= H:
        continue                          # this turn misses the material
    body = body.cut(one_turn.translate(cq.Vector(0, 0, zs)))

# the thread stops at the floor of the bottom counterbore: refill the groove
# below the floor, then bore the counterbore
fill = cylinder(R_CORE - 0.05, 0.0, CB_DEPTH, SEAM_IN).cut(
    cylinder(CB_D / 2.0 - 0.05, -1.0, CB_DEPTH + 2.0, SEAM_IN)
)
body = body.union(cq.Workplane("XY").add(fill))
body = body.cut(cq.Workplane("XY").add(cylinder(CB_D / 2.0, -1.0, CB_DEPTH + 1.0, SEAM_IN)))

result = body
